"""Reducing socket / spigot fitting (funnel-shaped pipe reducer).

A large, open socket (tapered bore, thin mouth) is joined by a conical
shoulder to a small spigot tube.  The inside follows the outside: the
socket bore ends in an inner cone that runs parallel to the outer cone
and blends into the spigot bore.  The part is a single revolved profile
around the X axis (socket opening towards +X), with small rounds on the
exposed edges.
"""
import cadquery as cq

# ---- driving dimensions (mm) ----
D_LARGE = 100.0      # outer diameter of the large socket
L_LARGE = 34.6       # length of the large cylindrical socket (outside)
L_CONE = 23.0        # axial length of the conical shoulder (outside)
D_SMALL = 48.0       # outer diameter of the small spigot
L_SMALL = 53.4       # length of the small spigot (outside)

D_BORE = 40.5        # spigot bore where it meets the inner cone (narrowest)
D_BORE_END = 41.2    # spigot bore at its open end (slight core draft)

T_RIM = 2.3          # wall thickness at the socket mouth
T_SOCK = 4.0         # wall thickness at the socket bottom (tapered socket bore)
SOCKET_DEPTH = 28.7  # socket depth, mouth to start of the inner cone

F_EDGE = 0.5         # small round on the outer / end edges
F_BORE = 1.0         # blend between inner cone and spigot bore
SEAM_ANGLE = 235.0   # angular position of the revolve seam (cosmetic only)

# ---- derived profile ----
R_L = D_LARGE / 2
R_S = D_SMALL / 2
R_B = D_BORE / 2
R_BE = D_BORE_END / 2

x0 = 0.0                              # spigot end
x1 = L_SMALL                          # spigot / shoulder
x2 = L_SMALL + L_CONE                 # shoulder / socket
x3 = L_SMALL + L_CONE + L_LARGE       # socket mouth

R_IN_TOP = R_L - T_RIM                # socket bore radius at the mouth
R_IN_BOT = R_L - T_SOCK               # socket bore radius at its bottom
xi_top = x3 - SOCKET_DEPTH            # socket bottom = start of inner cone
k_cone = (R_L - R_S) / L_CONE         # outer cone slope dr/dx
xi_bot = xi_top - (R_IN_BOT - R_B) / k_cone   # inner cone (parallel) meets bore

profile = [
    (x0, R_BE),
    (x0, R_S),
    (x1, R_S),
    (x2, R_L),
    (x3, R_L),
    (x3, R_IN_TOP),
    (xi_top, R_IN_BOT),
    (xi_bot, R_B),
]

# half cross-section in the XY plane (Y = radius), revolved about the X axis
body = (
    cq.Workplane("XY")
    .polyline(profile)
    .close()
    .revolve(360, (0, 0, 0), (1, 0, 0))
)


class RingEdge(cq.Selector):
    """Select the circular edge centred on the X axis at axial position x with radius r."""

    def __init__(self, x, r, tol=0.05):
        self.x, self.r, self.tol = x, r, tol

    def filter(self, objs):
        out = []
        for e in objs:
            if e.geomType() != "CIRCLE":
                continue
            c = e.Center()
            if abs(c.x - self.x) < self.tol and abs(e.radius() - self.r) < self.tol:
                out.append(e)
        return out


# blend where the inner cone runs into the spigot bore
body = body.edges(RingEdge(xi_bot, R_B)).fillet(F_BORE)

# small rounds: spigot end (inside + outside), both shoulder corners,
# socket mouth (outside + inside)
for xe, re in [(x0, R_BE), (x0, R_S), (x1, R_S), (x2, R_L), (x3, R_L), (x3, R_IN_TOP)]:
    body = body.edges(RingEdge(xe, re)).fillet(F_EDGE)

# centre the part along its axis; turn the seam away from the main view
result = (
    body.rotate((0, 0, 0), (1, 0, 0), SEAM_ANGLE)
    .translate((-x3 / 2, 0, 0))
)

VIEW = {"azimuth": 45, "elevation": 26}
